import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# main frame plate
PLATE_W = 164.6          # along X
PLATE_D = 139.9          # along Y
PLATE_T = 4.6            # thickness
PLATE_CORNER_R = 3.0     # vertical corner rounds
PLATE_EDGE_R = 1.5       # top perimeter round (bottom edge stays sharp)

HOLE_PX = 147.6          # corner hole pitch X
HOLE_PY = 123.5          # corner hole pitch Y
HOLE_D = 6.5

# tapered rectangular window
WIN_TOP_W = 90.8
WIN_TOP_D = 70.3
WIN_BOT_W = 80.8
WIN_BOT_D = 60.1

# blocks under the plate
BLK_H = 9.9              # depth below the plate
BLK_CX = 3.0             # block pattern centre offset X
BLK_CY = 1.5             # block pattern centre offset Y
PAD_L = 24.5             # pad length (X)
PAD_W = 12.0             # pad width (Y)
PAD_HOLE_PX = 93.2       # tapped-hole pitch X
PAD_HOLE_PY = 97.0       # tapped-hole pitch Y
PAD_HOLE_D = 6.0
PAD_HOLE_DEPTH = 8.0
RIB_T = 6.85             # thickness of L rib (X)
L_RIB_LEN = 36.4         # length of L rib along Y
L_CORNER_R = 2.5
E_LEN = 16.8             # small centre block (left side) length along Y

# clamp bars
BAR_L = 118.2
BAR_W = 13.2
BAR_H = 7.8
BAR_CX = 2.7
BAR_Y_BACK = 107.7
BAR_Y_FRONT = -116.4
BAR_HOLE_P = 93.3
BAR_HOLE_D = 6.6
BAR_HOLE_OUT = 0.8       # holes sit slightly outboard of the bar centre line

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY")
    .rect(PLATE_W, PLATE_D)
    .extrude(PLATE_T)
    .edges("|Z").fillet(PLATE_CORNER_R)
)
plate = plate.faces(">Z").edges().fillet(PLATE_EDGE_R)

# tapered window (2-section loft)
win = (
    cq.Workplane("XY").workplane(offset=-0.5)
    .rect(WIN_BOT_W - (WIN_TOP_W - WIN_BOT_W) / PLATE_T * 0.5,
          WIN_BOT_D - (WIN_TOP_D - WIN_BOT_D) / PLATE_T * 0.5)
    .workplane(offset=PLATE_T + 1.0)
    .rect(WIN_TOP_W + (WIN_TOP_W - WIN_BOT_W) / PLATE_T * 0.5,
          WIN_TOP_D + (WIN_TOP_D - WIN_BOT_D) / PLATE_T * 0.5)
    .loft()
)
plate = plate.cut(win)

# corner holes
plate = (
    plate.faces(">Z").workplane()
    .rect(HOLE_PX, HOLE_PY, forConstruction=True).vertices()
    .hole(HOLE_D)
)

# ---------------- blocks under plate ----------------
def box(x0, x1, y0, y1):
    return (
        cq.Workplane("XY").workplane(offset=-BLK_H)
        .center((x0 + x1) / 2.0, (y0 + y1) / 2.0)
        .rect(abs(x1 - x0), abs(y1 - y0))
        .extrude(BLK_H + 0.5)
    )

hx = PAD_HOLE_PX / 2.0
hy = PAD_HOLE_PY / 2.0
blocks = []
# left pads (front and back)
for sy in (-1, 1):
    cy = BLK_CY + sy * hy
    cx = BLK_CX - hx
    blocks.append(box(cx - PAD_L / 2, cx + PAD_L / 2, cy - PAD_W / 2, cy + PAD_W / 2))
# left small centre block
ex1 = BLK_CX - hx - PAD_L / 2
blocks.append(box(ex1 - RIB_T, ex1, -E_LEN / 2, E_LEN / 2))
# right L brackets
for sy in (-1, 1):
    cy = BLK_CY + sy * hy
    cx = BLK_CX + hx
    x0 = cx - PAD_L / 2
    x1 = cx + PAD_L / 2
    yo = cy + sy * PAD_W / 2          # outer y of pad
    yi = yo - sy * L_RIB_LEN          # inner end of rib
    pad = box(x0, x1 + RIB_T, cy - PAD_W / 2, cy + PAD_W / 2)
    rib = box(x1, x1 + RIB_T, min(yo, yi), max(yo, yi))
    L = pad.union(rib)
    # round the outer corner vertical edge
    L = L.edges("|Z").edges(
        cq.selectors.NearestToPointSelector((x1 + RIB_T, yo, -BLK_H / 2))
    ).fillet(L_CORNER_R)
    blocks.append(L)

for b in blocks:
    plate = plate.union(b)

# tapped holes in the pads (blind, from below)
pad_pts = [
    (BLK_CX + sx * hx, BLK_CY + sy * hy) for sx in (-1, 1) for sy in (-1, 1)
]
for x, y in pad_pts:
    plate = plate.cut(
        cq.Workplane("XY").workplane(offset=-BLK_H - 0.1)
        .center(x, y).circle(PAD_HOLE_D / 2).extrude(PAD_HOLE_DEPTH + 0.1)
    )

# ---------------- clamp bars ----------------
def bar(yc):
    b = (
        cq.Workplane("XY").workplane(offset=PLATE_T - BAR_H)
        .center(BAR_CX, yc)
        .rect(BAR_L, BAR_W)
        .extrude(BAR_H)
    )
    yh = yc + (BAR_HOLE_OUT if yc > 0 else -BAR_HOLE_OUT)
    holes = (
        cq.Workplane("XY").workplane(offset=PLATE_T - BAR_H - 1.0)
        .pushPoints([(BAR_CX - BAR_HOLE_P / 2, yh), (BAR_CX + BAR_HOLE_P / 2, yh)])
        .circle(BAR_HOLE_D / 2)
        .extrude(BAR_H + 2.0)
    )
    return b.cut(holes)

result = plate.union(bar(BAR_Y_BACK)).union(bar(BAR_Y_FRONT))
